import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# Flanged wall-mount enclosure base.
# Coordinates: X right, Z up, Y back.  The flat mounting face (back of the
# flange and of the box) lies on Y = 0, the open rim faces -Y (front).
# ---------------------------------------------------------------------------

# --- main box -------------------------------------------------------------
BOX_W = 100.0          # outer width  (X)
BOX_H = 159.4          # outer height (Z)
BOX_D = 54.95          # depth of box from mounting face to rim face
BOX_R = 5.5            # radius of the box corner edges (parallel to Y)
RIM_EDGE_FILLET = 0.5  # small round on the outer rim edge

# --- cavity ---------------------------------------------------------------
CAV_W = 83.8
CAV_H = 142.6
CAV_R = 5.7            # cavity corner radius
BACK_WALL = 4.0        # thickness of the back wall
CAV_FILLET = 1.0       # fillet between cavity walls and back wall

# --- rim tongue -----------------------------------------------------------
TONGUE_IN = 2.8        # tongue outer edge, inset from outer wall
TONGUE_W = 3.0         # tongue width
TONGUE_H = 0.45        # tongue height above rim face
TONGUE_ROUND = 0.4     # round-over of the tongue crest

# --- mounting flange -----------------------------------------------------
FL_T = 2.7             # flange thickness
EAR_HX = 52.4          # ear hole centres (+-X)
EAR_HZ = 82.1          # ear hole centres (+-Z)
EAR_HOLE_D = 4.0
EAR_X = 56.8           # outer extent of the ears in X
EAR_Z = 86.6           # outer extent of the ears in Z
EAR_TIP_R = 2.8        # corner radius at the ear tip
LOBE_X = 59.3          # outer extent of side lobes
LOBE_FLAT = 6.0        # half length of flat part of lobe
SLOT_X = 54.55         # slot centre (+-X)
SLOT_W = 3.9
SLOT_H = 10.7

# --- internal bosses -----------------------------------------------------
BOSS_X = 20.3
BOSS_Z = 27.5
BOSS_D = 10.9
BOSS_LEN = 7.0         # height above back wall
BOSS_FILLET = 3.0      # blend radius at the boss root
BOSS_HOLE_D = 3.8
BOSS_HOLE_DEPTH = 6.5

# --- snap beads on inner side walls -------------------------------------
BEAD_BASE = 4.3       # width of the bead along Y
BEAD_H = 2.15         # how far the bead stands off the wall
BEAD_HALF_LEN = 16.7

half_w = BOX_W / 2.0
half_h = BOX_H / 2.0


def rounded_polygon(pts, radii):
    """Closed XZ-plane wire (on Workplane 'XZ') of straight segments with a
    tangent fillet arc of the given radius at each vertex (0 = sharp)."""
    n = len(pts)
    segs = []  # list of (T1, M, T2) or (P,) for each vertex
    for i in range(n):
        p0 = pts[i - 1]
        p1 = pts[i]
        p2 = pts[(i + 1) % n]
        r = radii[i]
        if r <= 0:
            segs.append((p1,))
            continue
        d1 = (p1[0] - p0[0], p1[1] - p0[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (p2[0] - p1[0], p2[1] - p1[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        theta = math.acos(cosang)
        s = r * math.tan(theta / 2.0)
        t1 = (p1[0] - d1[0] * s, p1[1] - d1[1] * s)
        t2 = (p1[0] + d2[0] * s, p1[1] + d2[1] * s)
        cross = d1[0] * d2[1] - d1[1] * d2[0]
        # normal of d1 pointing to the inside of the turn
        if cross > 0:
            nrm = (-d1[1], d1[0])
        else:
            nrm = (d1[1], -d1[0])
        c = (t1[0] + nrm[0] * r, t1[1] + nrm[1] * r)
        v = (p1[0] - c[0], p1[1] - c[1])
        lv = math.hypot(*v)
        m = (c[0] + v[0] / lv * r, c[1] + v[1] / lv * r)
        segs.append((t1, m, t2))

    first = segs[0]
    start = first[2] if len(first) == 3 else first[0]
    wp = cq.Workplane("XZ").moveTo(*start)
    cur = start
    for i in list(range(1, n)) + [0]:
        sg = segs[i]
        tgt = sg[0]
        if math.hypot(tgt[0] - cur[0], tgt[1] - cur[1]) > 1e-6:
            wp = wp.lineTo(*tgt)
        if len(sg) == 3:
            wp = wp.threePointArc(sg[1], sg[2])
            cur = sg[2]
        else:
            cur = tgt
    return wp.close()


# ---------------------------------------------------------------------------
# flange outline (counter-clockwise, starting top middle going left)
# ---------------------------------------------------------------------------
# S-shaped blends (two tangent arcs) between the ears / lobes and the box
EAR_TOP_FLAT_END = 49.5   # x where the flat ear top starts to blend down
EAR_TOP_BLEND_END = 33.5  # x where the blend meets the box top edge
EAR_SIDE_FLAT_END = 78.5  # z where the flat ear side starts to blend in
EAR_SIDE_BLEND_END = 63.0 # z where the blend meets the box side
LOBE_BLEND_END = 28.0     # z where the lobe blend meets the box side


def s_blend(h, run):
    """Radius and vertex setback of an S-blend (two equal tangent arcs)
    bridging two parallel lines offset by h over a length run."""
    half = math.atan2(h, run)          # half of the turning angle
    phi = 2.0 * half
    r = run / (2.0 * math.sin(phi))
    return r, r * math.tan(half)


r_et, s_et = s_blend(EAR_Z - half_h, EAR_TOP_FLAT_END - EAR_TOP_BLEND_END)
r_es, s_es = s_blend(EAR_X - half_w, EAR_SIDE_FLAT_END - EAR_SIDE_BLEND_END)
r_lb, s_lb = s_blend(LOBE_X - half_w, LOBE_BLEND_END - LOBE_FLAT)

quarter = [  # top-left quarter, from top middle towards the left side
    ((-(EAR_TOP_BLEND_END + s_et), half_h), r_et),
    ((-(EAR_TOP_FLAT_END - s_et), EAR_Z), r_et),
    ((-EAR_X, EAR_Z), EAR_TIP_R),
    ((-EAR_X, EAR_SIDE_FLAT_END - s_es), r_es),
    ((-half_w, EAR_SIDE_BLEND_END + s_es), r_es),
    ((-half_w, LOBE_BLEND_END - s_lb), r_lb),
    ((-LOBE_X, LOBE_FLAT + s_lb), r_lb),
]
# left side: top-left quarter + mirrored bottom-left quarter
left = quarter + [((x, -z), r) for (x, z), r in reversed(quarter)]
# right side: mirror of the left side in X, traversed upward
right = [((-x, z), r) for (x, z), r in reversed(left)]
outline = left + right
pts = [p for p, r in outline]
rad = [r for p, r in outline]

flange = rounded_polygon(pts, rad).extrude(FL_T)

# ear holes and side slots through the flange
hole_pts = [(sx * EAR_HX, sz * EAR_HZ) for sx in (-1, 1) for sz in (-1, 1)]
ear_holes = (cq.Workplane("XZ").pushPoints(hole_pts)
             .circle(EAR_HOLE_D / 2.0).extrude(FL_T))
slots = (cq.Workplane("XZ").pushPoints([(-SLOT_X, 0), (SLOT_X, 0)])
         .rect(SLOT_W, SLOT_H).extrude(FL_T)
         .edges("|Y").fillet(0.6))
flange = flange.cut(ear_holes).cut(slots)

# ---------------------------------------------------------------------------
# box shell
# ---------------------------------------------------------------------------
box = (cq.Workplane("XZ").rect(BOX_W, BOX_H).extrude(BOX_D)
       .edges("|Y").fillet(BOX_R))
box = box.faces("<Y").edges().fillet(RIM_EDGE_FILLET)

body = flange.union(box)

# raised tongue on the rim face
tongue = (cq.Workplane("XZ", origin=(0, -BOX_D, 0))
          .sketch()
          .rect(BOX_W - 2 * TONGUE_IN, BOX_H - 2 * TONGUE_IN)
          .vertices().fillet(BOX_R - TONGUE_IN)
          .reset()
          .rect(BOX_W - 2 * (TONGUE_IN + TONGUE_W),
                BOX_H - 2 * (TONGUE_IN + TONGUE_W), mode="s")
          .reset()
          .finalize()
          .extrude(TONGUE_H)
          .faces("<Y").edges().fillet(TONGUE_ROUND))
body = body.union(tongue)

# cavity
cav_depth = BOX_D + TONGUE_H + 1.0 - BACK_WALL
cavity = (cq.Workplane("XZ", origin=(0, -(BOX_D + TONGUE_H + 1.0), 0))
          .rect(CAV_W, CAV_H).extrude(-cav_depth)
          .edges("|Y").fillet(CAV_R)
          .faces(">Y").edges().fillet(CAV_FILLET))
body = body.cut(cavity)

# ---------------------------------------------------------------------------
# internal screw bosses on the back wall
# ---------------------------------------------------------------------------
boss_pts = [(-BOSS_X, BOSS_Z), (BOSS_X, BOSS_Z)]
for bx, bz in boss_pts:
    # boss with a fillet-like root: revolve a profile around the boss axis
    rb = BOSS_D / 2.0
    rf = BOSS_FILLET
    prof = (cq.Workplane("XY")
            .moveTo(0, 0)
            .lineTo(rb + rf, 0)
            .radiusArc((rb, -rf), -rf)
            .lineTo(rb, -BOSS_LEN)
            .lineTo(0, -BOSS_LEN)
            .close())
    boss = prof.revolve(360, (0, 0, 0), (0, 1, 0))
    boss = boss.translate((bx, -BACK_WALL, bz))
    body = body.union(boss)
boss_holes = (cq.Workplane("XZ", origin=(0, -(BACK_WALL + BOSS_LEN), 0))
              .pushPoints(boss_pts).circle(BOSS_HOLE_D / 2.0)
              .extrude(-BOSS_HOLE_DEPTH))
body = body.cut(boss_holes)

# ---------------------------------------------------------------------------
# snap beads on the inner side walls, right at the rim
# ---------------------------------------------------------------------------
for sx in (-1, 1):
    xw = sx * CAV_W / 2.0             # inner face of the side wall
    d = -sx                           # direction pointing into the cavity
    y0 = -BOX_D                       # bead starts at the rim face
    y1 = y0 + BEAD_BASE               # ... and ends BEAD_BASE behind it
    ym = 0.5 * (y0 + y1)
    tri = (cq.Workplane("XY", origin=(0, 0, -BEAD_HALF_LEN))
           .polyline([(xw - d * 0.5, y0), (xw - d * 0.5, y1),
                      (xw + d * BEAD_H, ym)]).close()
           .extrude(2 * BEAD_HALF_LEN))
    # trapezoid in XZ giving 45 deg end chamfers
    L = BEAD_HALF_LEN
    e = BEAD_H + 0.5
    trap_pts = [(xw - d * 1.0, -L - 1.0), (xw + d * e, -L + e),
                (xw + d * e, L - e), (xw - d * 1.0, L + 1.0)]
    trap = (cq.Workplane("XZ", origin=(0, y0 - 0.5, 0))
            .polyline(trap_pts).close().extrude(-(BEAD_BASE + 1.0)))
    bead = tri.intersect(trap)
    body = body.union(bead)

result = body
